import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 120.0          # plate width (square)
T = 2.0            # plate thickness
C = 15.7           # corner block size (square)
H = 14.0           # corner block height (from plate bottom)
MAG_D = 10.0       # blind hole under each block (from below)
MAG_DEPTH = 4.0
MAG_INSET = 9.0    # hole centre distance from the plate edges
HOLE_D = 3.5       # small through holes at edge mid-points
HOLE_INSET = C / 2 # hole centre distance from plate edge

TEXT = "CUBINO"
TEXT_FONT = "DejaVu Sans"
TEXT_SIZE = 0.08 * W     # font size
TEXT_STRETCH = 0.95      # horizontal scale of the lettering
TEXT_Y = 0.237 * W       # text centre (Y), text reads from the +Y side
TEXT_DEPTH = 0.8

LOGO_SCALE = W / 120.0   # toucan outline points below are drawn for W = 120
LOGO_GROOVE_W = 0.45     # width of the engraved logo outline
LOGO_DEPTH = 0.4

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- plate ----------------
plate = cq.Workplane("XY").box(W, W, T, centered=(True, True, False))

# corner blocks
off = W / 2 - C / 2
corners = [(sx * off, sy * off) for sx in (-1, 1) for sy in (-1, 1)]
blocks = cq.Workplane("XY").pushPoints(corners).rect(C, C).extrude(H)
body = plate.union(blocks)

# blind holes from below under the blocks
mo = W / 2 - MAG_INSET
mag_pts = [(sx * mo, sy * mo) for sx in (-1, 1) for sy in (-1, 1)]
mags = cq.Workplane("XY").pushPoints(mag_pts).circle(MAG_D / 2).extrude(MAG_DEPTH)
body = body.cut(mags)

# small through holes at edge mid-points
hp = W / 2 - HOLE_INSET
holes = (
    cq.Workplane("XY")
    .pushPoints([(0, hp), (0, -hp), (hp, 0), (-hp, 0)])
    .circle(HOLE_D / 2)
    .extrude(T + 1)
    .translate((0, 0, -0.5))
)
body = body.cut(holes)

# engraved lettering on the top face (upside down, i.e. rotated 180 deg about Z,
# and horizontally stretched to match the wide type face)
glyphs = cq.Compound.makeText(TEXT, TEXT_SIZE, 1.0, font=TEXT_FONT, kind="bold",
                               halign="center", valign="center")
xform = cq.Matrix([[-TEXT_STRETCH, 0, 0, 0], [0, -1, 0, TEXT_Y], [0, 0, 1, 0]])
txt_solids = []
for f in glyphs.Faces():
    if f.normalAt().z > -0.99 or abs(f.Center().z) > 1e-6:
        continue  # keep only the flat bottom faces of the glyphs
    outer = f.outerWire().transformGeometry(xform)
    inners = [w.transformGeometry(xform) for w in f.innerWires()]
    flat = cq.Face.makeFromWires(outer, inners)
    sol = cq.Solid.extrudeLinear(flat, cq.Vector(0, 0, TEXT_DEPTH + 0.5))
    txt_solids.append(sol.translate(cq.Vector(0, 0, T - TEXT_DEPTH)))
txt_cut = cq.Workplane("XY").add(cq.Compound.makeCompound(txt_solids))
body = body.cut(txt_cut)

# ---------------- engraved toucan logo (outline grooves) ----------------
# closed outlines (mm, plate coordinates)
LOGO_BEAK = [(-6.04, -26.05), (-5.4, -24.63), (-3.83, -23.92), (-1.8, -23.62),
             (-0.38, -23.47), (-0.56, -24.74), (-0.94, -26.31), (-2.26, -26.21),
             (-4.14, -26.36), (-5.71, -26.61)]
LOGO_BODY = [(-0.38, -23.47), (1.17, -23.23), (2.26, -24.03), (2.58, -25.58),
             (2.41, -26.82), (2.71, -27.63), (3.48, -29.05), (3.56, -31.18),
             (3.37, -33.46), (3.56, -34.68), (3.73, -35.9), (3.42, -36.33),
             (0.74, -36.28), (0.58, -35.3), (0.38, -34.2), (-1.01, -33.46),
             (-2.24, -32.04), (-2.77, -30.3), (-2.61, -28.95), (-2.16, -27.78),
             (-1.29, -26.77), (-0.89, -24.99)]
# open strokes
LOGO_WING = [(-1.34, -27.78), (-0.08, -28.39), (0.53, -29.35), (0.89, -30.57),
             (1.09, -32.04), (0.92, -33.82), (0.43, -34.43)]
LOGO_BEAK_LINE = [(-5.15, -25.75), (-3.93, -25.6), (-2.66, -25.5), (-0.94, -25.29)]
LOGO_EYE = (0.38, -25.65)
LOGO_EYE_R = 0.5


def sc(pts):
    return [(x * LOGO_SCALE, y * LOGO_SCALE) for x, y in pts]


def offset_pts(pts, d):
    """Offset a closed point loop by d along its outward vertex normals."""
    n = len(pts)
    area = sum(pts[i][0] * pts[(i + 1) % n][1] - pts[(i + 1) % n][0] * pts[i][1] for i in range(n))
    sgn = 1.0 if area > 0 else -1.0
    out = []
    for i in range(n):
        px, py = pts[i - 1]
        nx_, ny_ = pts[(i + 1) % n]
        tx, ty = nx_ - px, ny_ - py
        ln = (tx * tx + ty * ty) ** 0.5
        out.append((pts[i][0] + sgn * d * ty / ln, pts[i][1] - sgn * d * tx / ln))
    return out


def closed_spline(pts):
    vs = [cq.Vector(x, y, 0) for x, y in pts]
    return cq.Wire.assembleEdges([cq.Edge.makeSpline(vs, periodic=True)])


def closed_groove(pts, width, depth, z_top):
    outer = closed_spline(offset_pts(pts, width / 2))
    inner = closed_spline(offset_pts(pts, -width / 2))
    face = cq.Face.makeFromWires(outer, [inner])
    solid = cq.Solid.extrudeLinear(face, cq.Vector(0, 0, depth + 0.5))
    return solid.translate(cq.Vector(0, 0, z_top - depth))


def open_groove(pts, width, depth, z_top):
    """Rectangular groove swept along an open spline stroke."""
    z0 = z_top - depth
    vs = [cq.Vector(x, y, z0) for x, y in pts]
    edge = cq.Edge.makeSpline(vs)
    t0 = edge.tangentAt(0)
    t0 = cq.Vector(t0.x, t0.y, 0).normalized()
    plane = cq.Plane(origin=vs[0], xDir=cq.Vector(-t0.y, t0.x, 0), normal=t0)
    hgt = depth + 0.5
    prof = cq.Workplane(plane).center(0, hgt / 2).rect(width, hgt).val()
    return cq.Solid.sweep(prof, [], edge, True, False)


logo_cuts = [
    closed_groove(sc(LOGO_BEAK), LOGO_GROOVE_W, LOGO_DEPTH, T),
    closed_groove(sc(LOGO_BODY), LOGO_GROOVE_W, LOGO_DEPTH, T),
    open_groove(sc(LOGO_WING), LOGO_GROOVE_W, LOGO_DEPTH, T),
    open_groove(sc(LOGO_BEAK_LINE), LOGO_GROOVE_W * 0.8, LOGO_DEPTH, T),
]
eye_ring = (
    cq.Workplane("XY")
    .workplane(offset=T - LOGO_DEPTH)
    .center(*sc([LOGO_EYE])[0])
    .circle(LOGO_EYE_R * LOGO_SCALE + LOGO_GROOVE_W * 0.4)
    .circle(LOGO_EYE_R * LOGO_SCALE - LOGO_GROOVE_W * 0.4)
    .extrude(LOGO_DEPTH + 0.5)
)
logo_cuts.append(eye_ring.val())

for s_ in logo_cuts:
    body = body.cut(cq.Workplane("XY").add(s_))

result = body
